import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# origin: centre of the front (socket) face, socket opens towards -Y, Z up
L = 53.9            # body length along Y (front face y=0 -> back face y=L)

# front cross-section of the body (rounded rectangle)
FX0, FX1 = -25.0, 25.0
FZ0, FZ1 = -29.6, 29.6
# back cross-section (body flares towards the back, mostly on +X / -Z)
BX0, BX1 = -25.7, 28.6
BZ0, BZ1 = -32.3, 31.1
R_BODY = 10.0       # longitudinal corner radius of the body
MID_T = 0.5         # position of the middle loft section (fraction of L)
MID_F = 0.25        # fraction of the flare reached at the middle section

# socket (blind rectangular pocket from the front face)
SX0, SX1 = -18.2, 18.5
SZ0, SZ1 = -22.8, 22.6
SOCKET_D = 47.0
MOUTH_R = 2.0       # rounded lead-in on the +X edge of the socket mouth

# mounting tabs (flush with the back face)
TAB_Y0 = 30.9                    # front face of the tabs
TAB_R = 6.0                      # outer corner radius of the tabs
TT_X = (-13.4, 13.8)             # top / bottom tab width
TOP_Z1 = 47.8                    # top of top tab
BOT_Z0 = -52.2                   # bottom of bottom tab
SIDE_Z = (-18.25, 18.25)         # side tab height
LEFT_X0 = -43.2                  # outer face of -X tab
RIGHT_X1 = 48.0                  # outer face of +X tab

# back pad
PAD_X = (-18.5, 21.8)
PAD_Z = (-25.4, 24.3)
PAD_T = 6.7
PAD_R = 2.0

# holes
HOLE_D = 5.0
CB_D = 9.7           # tab hole counterbore
SIDE_CB_D = 10.2     # side hole counterbore
TAB_CB_DEPTH = 15.0
SIDE_CB_DEPTH = 2.5
SIDE_HOLE_Y = 11.3
SIDE_HOLE_Z = 13.6
TOP_HOLES = [(-6.8, 39.5), (6.9, 39.5)]
BOT_HOLES = [(0.1, -44.8)]
LEFT_HOLES = [(-34.1, 9.1), (-34.1, -8.9)]
RIGHT_HOLES = [(38.4, 9.1), (38.4, -8.9)]


# ---------------- helpers ----------------
def rrect_wire(x0, x1, z0, z1, r, y):
    V = cq.Vector
    c = 0.29289321881345254 * r  # r*(1-cos45)
    e = [
        cq.Edge.makeLine(V(x0 + r, y, z0), V(x1 - r, y, z0)),
        cq.Edge.makeThreePointArc(V(x1 - r, y, z0), V(x1 - c, y, z0 + c), V(x1, y, z0 + r)),
        cq.Edge.makeLine(V(x1, y, z0 + r), V(x1, y, z1 - r)),
        cq.Edge.makeThreePointArc(V(x1, y, z1 - r), V(x1 - c, y, z1 - c), V(x1 - r, y, z1)),
        cq.Edge.makeLine(V(x1 - r, y, z1), V(x0 + r, y, z1)),
        cq.Edge.makeThreePointArc(V(x0 + r, y, z1), V(x0 + c, y, z1 - c), V(x0, y, z1 - r)),
        cq.Edge.makeLine(V(x0, y, z1 - r), V(x0, y, z0 + r)),
        cq.Edge.makeThreePointArc(V(x0, y, z0 + r), V(x0 + c, y, z0 + c), V(x0 + r, y, z0)),
    ]
    return cq.Wire.assembleEdges(e)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def lerp(a, b, t):
    return a + (b - a) * t


# ---------------- body (flared loft) ----------------
mid = [lerp(f, b, MID_F) for f, b in zip((FX0, FX1, FZ0, FZ1), (BX0, BX1, BZ0, BZ1))]
w_front = rrect_wire(FX0, FX1, FZ0, FZ1, R_BODY, 0.0)
w_mid = rrect_wire(mid[0], mid[1], mid[2], mid[3], R_BODY, L * MID_T)
w_back = rrect_wire(BX0, BX1, BZ0, BZ1, R_BODY, L)
body = cq.Workplane("XY").add(cq.Solid.makeLoft([w_front, w_mid, w_back], False))

# ---------------- tabs ----------------
# each tab is a block running from TAB_Y0 to the back face; its inner end is
# buried in the body wall (anything inside the socket is removed later)
TAB_IN = 15.0
top_tab = box(TT_X[0], TT_X[1], TAB_Y0, L, TAB_IN, TOP_Z1).edges("|Y and >Z").fillet(TAB_R)
bot_tab = box(TT_X[0], TT_X[1], TAB_Y0, L, BOT_Z0, -TAB_IN).edges("|Y and <Z").fillet(TAB_R)
left_tab = box(LEFT_X0, -TAB_IN, TAB_Y0, L, SIDE_Z[0], SIDE_Z[1]).edges("|Y and <X").fillet(TAB_R)
right_tab = box(TAB_IN, RIGHT_X1, TAB_Y0, L, SIDE_Z[0], SIDE_Z[1]).edges("|Y and >X").fillet(TAB_R)

part = body.union(top_tab).union(bot_tab).union(left_tab).union(right_tab)

# ---------------- back pad ----------------
pad = box(PAD_X[0], PAD_X[1], L - 0.01, L + PAD_T, PAD_Z[0], PAD_Z[1])
pad = pad.faces(">Y").edges().fillet(PAD_R)
part = part.union(pad)

# ---------------- socket ----------------
part = part.cut(box(SX0, SX1, -1.0, SOCKET_D, SZ0, SZ1))
# rounded lead-in on the +X vertical edge of the socket mouth
part = part.edges(cq.selectors.BoxSelector((SX1 - 0.5, -0.5, SZ0 + 1.0),
                                           (SX1 + 0.5, 0.5, SZ1 - 1.0))).fillet(MOUTH_R)

# ---------------- side cross holes (along X) ----------------
for zc in (SIDE_HOLE_Z, -SIDE_HOLE_Z):
    thru = (cq.Workplane("YZ", origin=(-60, SIDE_HOLE_Y, zc))
            .circle(HOLE_D / 2).extrude(120))
    part = part.cut(thru)
    cb_r = (cq.Workplane("YZ", origin=(FX1 - SIDE_CB_DEPTH + 0.1, SIDE_HOLE_Y, zc))
            .circle(SIDE_CB_D / 2).extrude(15))
    cb_l = (cq.Workplane("YZ", origin=(FX0 + SIDE_CB_DEPTH - 0.05, SIDE_HOLE_Y, zc))
            .circle(SIDE_CB_D / 2).extrude(-15))
    part = part.cut(cb_r).cut(cb_l)

# ---------------- tab holes (along Y, counterbored from the front) ----------------
for (xc, zc) in TOP_HOLES + BOT_HOLES + LEFT_HOLES + RIGHT_HOLES:
    # XZ workplane normal is -Y, so negative extrusion goes towards +Y
    thru = (cq.Workplane("XZ", origin=(xc, TAB_Y0 - 1.0, zc))
            .circle(HOLE_D / 2).extrude(-(L - TAB_Y0 + 2.0)))
    cb = (cq.Workplane("XZ", origin=(xc, TAB_Y0 - 1.0, zc))
          .circle(CB_D / 2).extrude(-(TAB_CB_DEPTH + 1.0)))
    part = part.cut(thru).cut(cb)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
